import math
import cadquery as cq

# ---------------------------------------------------------------
# Tapered fender / guard: thin-walled shell arch with a raised hollow
# rail (hat channel) along the top, a flared +X skirt with a scalloped
# lower edge, a -X arch with a large rounded cut-out and a curved
# back trim.  X across, Y along the part (front Y=0 -> back Y=L), Z up.
# ---------------------------------------------------------------

L = 200.0          # overall length
T = 2.8            # wall thickness
RF = 1.5           # outer fillet at the rail / skirt corner

# sampling of the section curves (points per spline)
N_ARCH = 9
N_SKIRT_IN = 11
SKIRT_LEVELS = (1.0, 0.80, 0.62, 0.46, 0.32, 0.19, 0.08, 0.0)

# loft stations
#  Y, Z_rail, X_step, step_h, XL (outer left foot), arch centre (xc, zc), skirt blend w
STATIONS = [
    (0.0,   38.6, -18.0, 4.0, -54.3, -17.5,  0.0, 0.00),
    (50.0,  40.4, -19.1, 3.8, -64.6, -20.5, -1.7, 0.40),
    (100.0, 44.4, -20.1, 3.6, -74.8, -23.5, -3.4, 0.60),
    (150.0, 47.8, -20.8, 3.5, -80.6, -26.5, -5.0, 1.00),
    (200.0, 48.5, -21.3, 3.4, -81.1, -29.4, -6.7, 1.00),
]

# +X skirt profiles (X as function of Z): front end and rear part
FRONT_SKIRT = [(0.0, 16.4), (4.5, 15.3), (8.4, 13.8), (11.1, 12.4), (14.1, 11.0),
               (16.8, 9.6), (19.8, 7.9), (22.7, 5.4), (26.5, 2.3), (30.5, 0.7),
               (34.5, 0.15), (38.0, 0.0), (60.0, 0.0)]
BACK_SKIRT = [(0.0, 21.0), (3.7, 20.7), (6.0, 20.2), (11.8, 18.5), (15.1, 17.1),
              (18.4, 15.4), (21.7, 13.5), (24.1, 11.5), (26.6, 9.3), (29.1, 6.8),
              (31.5, 4.2), (34.0, 2.4), (36.0, 1.5), (38.0, 0.95), (42.0, 0.45),
              (46.0, 0.1), (60.0, 0.0)]


def interp(tab, z):
    if z <= tab[0][0]:
        return tab[0][1]
    for (z0, x0), (z1, x1) in zip(tab[:-1], tab[1:]):
        if z <= z1:
            return x0 + (x1 - x0) * (z - z0) / (z1 - z0)
    return tab[-1][1]


def skirt_x(z, w):
    return (1.0 - w) * interp(FRONT_SKIRT, z) + w * interp(BACK_SKIRT, z)


def ellipse_ab(xc, zc, XL, Xs, Zs):
    # axis aligned ellipse centred (xc, zc) through (XL, 0) and (Xs, Zs)
    a11, a12 = (XL - xc) ** 2, zc ** 2
    a21, a22 = (Xs - xc) ** 2, (Zs - zc) ** 2
    det = a11 * a22 - a12 * a21
    u = (a22 - a12) / det
    v = (a11 - a21) / det
    return 1.0 / math.sqrt(u), 1.0 / math.sqrt(v)


def build_wire(Y, Zr, Xs, hs, XL, xc, zc, w):
    Zs = Zr - hs
    a, b = ellipse_ab(xc, zc, XL, Xs, Zs)
    ai, bi = a - T, b - T

    def V(x, z):
        return cq.Vector(x, Y, z)

    # ---- left arch (outer / inner ellipses, concentric) ----
    def ell_pts(A, B, x_end, n):
        th0 = math.pi - math.asin(max(-1.0, min(1.0, -zc / B)))
        th1 = math.acos(max(-1.0, min(1.0, (x_end - xc) / A)))
        return [V(xc + A * math.cos(th0 + (th1 - th0) * i / (n - 1)),
                  zc + B * math.sin(th0 + (th1 - th0) * i / (n - 1))) for i in range(n)]

    arch_o = ell_pts(a, b, Xs, N_ARCH)
    arch_i = ell_pts(ai, bi, Xs + T, N_ARCH)
    arch_o[0] = V(arch_o[0].x, 0.0)
    arch_i[0] = V(arch_i[0].x, 0.0)
    Zs_i = arch_i[-1].z

    # ---- skirt: one smooth curve from the corner fillet down to the foot ----
    Zw = Zr - RF
    zs = [Zw * s for s in SKIRT_LEVELS]
    sk_o = [V(0.0, Zw)] + [V(skirt_x(z, w), z) for z in zs[1:]]
    e_sk_o = cq.Edge.makeSpline(sk_o, tangents=[cq.Vector(0, 0, -1), sk_o[-1] - sk_o[-2]])
    # inner skirt: offset of the outer curve by T
    n_i = N_SKIRT_IN
    sk_i = []
    for i in range(n_i):
        t = i / (n_i - 1.0)
        p = e_sk_o.positionAt(t)
        d = e_sk_o.tangentAt(t)
        nx, nz = -d.z, d.x          # outward normal of a downward running curve
        sk_i.append(V(p.x - T * nx, p.z - T * nz))
    # snap ends: top onto the inner rail roof, bottom onto z=0
    sk_i = [q for q in sk_i if q.z < Zr - T - 0.3]
    sk_i[0] = V(-T, Zr - T)
    p1, p2 = sk_i[-2], sk_i[-1]
    tt = (0.0 - p1.z) / (p2.z - p1.z)
    sk_i[-1] = V(p1.x + (p2.x - p1.x) * tt, 0.0)
    sk_i = list(reversed(sk_i))           # bottom -> top
    XR = sk_o[-1].x

    edges = [
        cq.Edge.makeSpline(arch_o),                                      # outer arch
        cq.Edge.makeLine(arch_o[-1], V(Xs, Zr)),                         # step
        cq.Edge.makeLine(V(Xs, Zr), V(-RF, Zr)),                         # rail top
        cq.Edge.makeThreePointArc(V(-RF, Zr),
                                  V(-RF + RF * math.sin(math.pi / 4), Zr - RF + RF * math.cos(math.pi / 4)),
                                  V(0.0, Zr - RF)),                      # corner fillet
        e_sk_o,                                                          # outer wall + skirt
        cq.Edge.makeLine(V(XR, 0.0), sk_i[0]),                           # skirt foot
        cq.Edge.makeSpline(sk_i, tangents=[sk_i[1] - sk_i[0], cq.Vector(0, 0, 1)]),  # inner skirt + wall
        cq.Edge.makeLine(V(-T, Zr - T), V(Xs + T, Zr - T)),              # inner rail top
        cq.Edge.makeLine(V(Xs + T, Zr - T), V(Xs + T, Zs_i)),            # inner step
        cq.Edge.makeSpline(list(reversed(arch_i))),                      # inner arch
        cq.Edge.makeLine(arch_i[0], arch_o[0]),                          # arch foot
    ]
    return cq.Wire.assembleEdges(edges)


def loft(wires, max_degree=3):
    from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
    bld = BRepOffsetAPI_ThruSections(True, False)
    bld.SetMaxDegree(max_degree)
    for wi in wires:
        bld.AddWire(wi.wrapped)
    bld.Build()
    return cq.Solid(bld.Shape())


wires = [build_wire(*s) for s in STATIONS]
body = cq.Workplane("XY").add(loft(wires))

# ---- +X skirt lower edge (side profile, everything below it removed) ----
SKIRT_EDGE = [
    (21.0, 0.0), (22.6, 3.6), (25.6, 7.2), (30.5, 10.9), (44.3, 17.0),
    (57.0, 20.2), (68.0, 20.9), (88.0, 17.6), (99.0, 13.2), (109.0, 10.1),
    (127.5, 3.4), (137.0, 4.6), (156.5, 16.4), (176.0, 27.5), (195.5, 31.0),
    (200.4, 34.0), (201.5, 38.0),
]
skirt_cut = (
    cq.Workplane("YZ", origin=(-8.0, 0, 0))
    .moveTo(20.6, -5.0)
    .lineTo(20.9, -1.0)
    .spline(SKIRT_EDGE, includeCurrent=True)
    .lineTo(212.0, 38.0)
    .lineTo(212.0, -5.0)
    .close()
    .extrude(80.0)
)
body = body.cut(skirt_cut)

# ---- -X arch cut-out (side profile, cut through the -X wall only) ----
ARCH_CUT = [
    (36.2, 0.0), (40.5, 6.8), (47.0, 13.4), (54.8, 18.9), (65.0, 24.8),
    (80.5, 29.5), (92.0, 30.5), (105.0, 28.5), (113.5, 24.2), (119.0, 18.0),
    (121.4, 10.0), (122.6, 0.0),
]
arch_cut = (
    cq.Workplane("YZ", origin=(-110.0, 0, 0))
    .moveTo(35.8, -5.0)
    .lineTo(36.1, -1.0)
    .spline(ARCH_CUT, includeCurrent=True)
    .lineTo(122.9, -5.0)
    .close()
    .extrude(80.0)          # spans X = -110 .. -30
)
body = body.cut(arch_cut)

# ---- -X back trim (plan curve, vertical cut) ----
TRIM = [
    (-22.0, 202.0), (-22.3, 200.0), (-24.9, 196.0), (-28.8, 190.1),
    (-38.7, 181.9), (-56.7, 175.0), (-76.0, 166.6), (-92.0, 154.0),
]
trim_cut = (
    cq.Workplane("XY", origin=(0, 0, -5.0))
    .moveTo(-22.0, 215.0)
    .lineTo(*TRIM[0])
    .spline(TRIM[1:], includeCurrent=True)
    .lineTo(-110.0, 154.0)
    .lineTo(-110.0, 215.0)
    .close()
    .extrude(80.0)
)
body = body.cut(trim_cut)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
